import cadquery as cq

# Open-ended U-channel enclosure half: base + two side walls (at +/-Y), U-shaped
# panel guide grooves at both open ends (+/-X), four screw bosses, vent slots
# and fixing holes in both walls.

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
L = 140.0          # length along X (open ends)
W = 121.0          # width along Y (walls at +/-Y)
H = 34.0           # overall height
T = 2.8            # wall / base thickness
R_OUT = 2.5        # outer bottom corner radius
R_IN = 3.0         # inner corner radius (main channel)

# end panel guide ribs (U-shaped, at both open ends)
RIB_P = 3.0        # rib protrusion from inner surface
RIB1_W = 2.9       # outer rib width (flush with end face)
GROOVE_W = 3.8     # panel groove width
RIB2_W = 2.9       # inner rib width
R_RIB = 2.7        # inner corner radius of the rib U

# bosses
BOSS_D = 11.4
BOSS_TOP = 14.0    # boss top height above underside
BOSS_FIL = 2.5
BOSS_HOLE_D = 4.0
BOSS_HOLE_DEPTH = 9.0
BOSS_X = (-56.2, 28.0)
BOSS_Y = 35.1

# wall holes
WH_D = 4.3
WH_X = 45.1
WH_Z = H - 6.4

# vent slots
SLOT_W = 2.2
SLOT_TOP = 17.0
SLOT_PITCH = 4.90
SLOT_N = 8
SLOT_X0 = L / 2 - 13.5       # outermost slot centre from centre (mirrored)
SLOT_IN = R_IN               # how far cut extends past inner wall face


def channel(thk, r_in, x0, x1):
    """U channel section (walls at +/-Y) extruded from x0 to x1."""
    ln = x1 - x0
    outer = (cq.Workplane("XY")
             .box(ln, W, H, centered=(False, True, False))
             .translate((x0, 0, 0))
             .edges("|X and <Z").fillet(R_OUT))
    inner = (cq.Workplane("XY")
             .box(ln + 2, W - 2 * thk, H + 5, centered=(False, True, False))
             .translate((x0 - 1, 0, thk))
             .edges("|X and <Z").fillet(r_in))
    return outer.cut(inner)


# main channel
body = channel(T, R_IN, -L / 2, L / 2)

# guide ribs at both ends
for s in (1, -1):
    xa = L / 2 - RIB1_W
    xb = L / 2
    xc = L / 2 - RIB1_W - GROOVE_W - RIB2_W
    xd = L / 2 - RIB1_W - GROOVE_W
    for (u0, u1) in ((xa, xb), (xc, xd)):
        lo, hi = sorted((s * u0, s * u1))
        body = body.union(channel(T + RIB_P, R_RIB, lo, hi))

# bosses
for bx in BOSS_X:
    for by in (BOSS_Y, -BOSS_Y):
        boss = (cq.Workplane("XY", origin=(bx, by, T - 0.5))
                .circle(BOSS_D / 2).extrude(BOSS_TOP - T + 0.5))
        body = body.union(boss)
        body = body.edges(cq.selectors.BoxSelector(
            (bx - BOSS_D, by - BOSS_D, T - 0.05),
            (bx + BOSS_D, by + BOSS_D, T + 0.05))).fillet(BOSS_FIL)
        hole = (cq.Workplane("XY", origin=(bx, by, BOSS_TOP - BOSS_HOLE_DEPTH))
                .circle(BOSS_HOLE_D / 2).extrude(BOSS_HOLE_DEPTH + 1))
        body = body.cut(hole)

# wall holes (through both walls)
for hx in (WH_X, -WH_X):
    cyl = (cq.Workplane("XZ", origin=(hx, W / 2 + 2, WH_Z))
           .circle(WH_D / 2).extrude(W + 4))
    body = body.cut(cyl)

# vent slots: rectangular cuts through each wall and the rounded corner below it
slot_len = SLOT_TOP + 3.0
slot_cz = SLOT_TOP - slot_len / 2
depth = T + SLOT_IN + 1.0
cutters = None
for sy in (1, -1):
    for gx in (1, -1):
        for i in range(SLOT_N):
            x = gx * (SLOT_X0 - i * SLOT_PITCH)
            if sy < 0:
                # front wall (-Y): XZ plane extrudes toward -Y, so start inside
                wp = cq.Workplane("XZ", origin=(x, -W / 2 + T + SLOT_IN, slot_cz))
            else:
                wp = cq.Workplane("XZ", origin=(x, W / 2 + 1.0, slot_cz))
            c = wp.rect(SLOT_W, slot_len).extrude(depth)
            cutters = c if cutters is None else cutters.union(c)
body = body.cut(cutters)

result = body
